import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# sausage (capsule along X, centred at origin)
SAUS_R = 31.8          # sausage radius
SAUS_L = 63.5          # half length of the cylindrical part

# bun: cylinder with a ball on each end, split lengthwise, the two halves
# opened like a clam shell about a hinge line behind the bun axis
BUN_R = 31.4           # bun radius (cylinder and end balls)
BUN_L = 71.5           # half length of the cylindrical part
BALL_LEFT = 5.95       # -X end: ball centre sits this far beyond the cylinder end
BALL_RIGHT = -0.65     # +X end: hemispherical cap centre relative to the nominal cylinder end
TOP_X = 0.85           # centre (X) of the upper half
BOT_X = -0.65          # centre (X) of the lower half
BUN_CY = 6.87          # closed-bun axis position (Y)
BUN_CZ = -5.6          # closed-bun axis position (Z)
HINGE_OFF = 24.0       # hinge line sits this far behind the bun axis (+Y)
OPEN_ANG = 45.0        # each half is opened by this angle

# mustard squiggle (thin plate standing in front of the sausage)
MUST_Y0 = -36.5        # front face
MUST_T = 2.9           # thickness

# loose slices (discs) floating above
DISC_R = 32.0
DISC_T = 3.4
# (x, y, z, tilt about X in degrees)
DISCS = [
    (-14.7, 22.5, 152.5, -22.3),
    (-1.5, 28.8, 136.8, 0.0),
    (-5.5, 38.9, 129.5, 0.0),
    (58.8, 38.9, 123.8, 0.0),
]


def cyl_x(r, x0, x1):
    """Cylinder along X from x0 to x1 (its seam line turned to the +Y side)."""
    c = cq.Solid.makeCylinder(r, x1 - x0, cq.Vector(0, 0, 0), cq.Vector(1, 0, 0))
    return c.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -90).translate(cq.Vector(x0, 0, 0))


def ball(r, xc):
    """Full ball centred on the X axis; poles on +-Y, seam meridian in the XY plane."""
    b = cq.Solid.makeSphere(r, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -90, 90, 360)
    return b.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90).translate(cq.Vector(xc, 0, 0))


def half_ball(r, xc, side):
    """Half ball on the side (side=+1: x >= xc, side=-1: x <= xc) of the plane x = xc."""
    b = cq.Solid.makeSphere(r, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -90, 90, 180)  # y >= 0 half
    b = b.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -90 * side)
    return b.translate(cq.Vector(xc, 0, 0))


def fuse(*shapes):
    wp = cq.Workplane("XY").add(shapes[0])
    for sh in shapes[1:]:
        wp = wp.union(cq.Workplane("XY").add(sh), clean=False)
    return wp


# ---------------- sausage ----------------
# two cylinder halves (seam at mid length) + a half ball on each end
sausage = fuse(cyl_x(SAUS_R, -SAUS_L, 0.0), cyl_x(SAUS_R, 0.0, SAUS_L),
               half_ball(SAUS_R, -SAUS_L, -1), half_ball(SAUS_R, SAUS_L, 1)).val().Solids()[0]

# ---------------- bun ----------------
# cylinder + a ball whose centre lies BALL_LEFT beyond the -X end (leaves a small
# shoulder at the cylinder end) + a tangent half ball at the +X end
xr = BUN_L + BALL_RIGHT
bun_full = fuse(cyl_x(BUN_R, -BUN_L, xr),
                ball(BUN_R, -BUN_L - BALL_LEFT),
                half_ball(BUN_R, xr, 1))
big = 400.0
upper = cq.Workplane("XY").box(big, big, big / 2, centered=(True, True, False))
lower = upper.translate((0, 0, -big / 2))
top_half = bun_full.intersect(upper)
bot_half = bun_full.intersect(lower)

hinge_a = cq.Vector(0, BUN_CY + HINGE_OFF, BUN_CZ)
hinge_b = hinge_a + cq.Vector(1, 0, 0)
top_half = top_half.translate((TOP_X, BUN_CY, BUN_CZ)).rotate(hinge_a, hinge_b, -OPEN_ANG)
bot_half = bot_half.translate((BOT_X, BUN_CY, BUN_CZ)).rotate(hinge_a, hinge_b, OPEN_ANG)

# ---------------- mustard squiggle ----------------
# outline of the squiggle in the XZ plane (front view)
MUST_PTS = [
    (-63.0, -8.5), (-58.5, -2.9), (-53.5, -4.4), (-43.5, 2.8), (-34.0, 5.0),
    (-25.0, 1.5), (-20.6, -10.4), (-14.5, -6.8), (-4.0, 3.2), (7.0, 3.8),
    (18.0, -1.0), (22.5, -9.5), (26.5, -9.8), (36.8, -0.5), (42.5, -4.0),
    (47.3, -9.6), (55.2, -2.8), (59.4, -8.0), (55.5, -17.5), (47.0, -23.0),
    (38.8, -16.4), (31.0, -21.0), (24.0, -23.3), (15.5, -19.0), (11.0, -10.6),
    (0.5, -9.6), (-10.5, -17.6), (-21.0, -23.7), (-29.0, -19.5), (-33.4, -8.8),
    (-40.5, -10.4), (-52.0, -17.8), (-60.5, -15.6),
]
mustard = (cq.Workplane("XZ", origin=(0, MUST_Y0 + MUST_T, 0))
           .spline(MUST_PTS, periodic=True, includeCurrent=False).close()
           .extrude(MUST_T))

# ---------------- discs ----------------
discs = []
for (x, y, z, tilt) in DISCS:
    d = (cq.Workplane("XZ", origin=(0, DISC_T / 2, 0)).circle(DISC_R).extrude(DISC_T)
         .rotate((0, 0, 0), (1, 0, 0), tilt).translate((x, y, z)))
    discs.append(d.val())

solids = [sausage] + top_half.val().Solids() + bot_half.val().Solids() + [mustard.val()] + discs
result = cq.Workplane("XY").add(cq.Compound.makeCompound(solids))

VIEW = {"azimuth": 45, "elevation": 26}
